import math
import cadquery as cq

VIEW = {"azimuth": 45, "elevation": 26}

# ---------------- driving dimensions (mm) ----------------
A_BULB = 44.3          # bulb: horizontal semi-axis of the elliptical bulb profile
B_BULB = 46.0          # bulb: vertical semi-axis
Z_BULB = 30.5          # height of bulb centre above the flat foot
H_TOTAL = 143.0        # overall height (foot to lip)
R_NECK_MIN = 15.3      # narrowest neck radius (neck is one concave arc tangent to the bulb)
Z_NECK_MIN = 128.7     # height of the narrowest neck section
R_HOLE = 10.5          # neck bore radius
Z_HOLE_BOTTOM = 30.0   # height of the flat bottom of the neck bore
R_DIMPLE = 1.5         # small centre mark in the foot
D_DIMPLE = 1.5

N_CUPS = 10            # egg cups per row (polar pattern)
A_CUP = 8.8            # cup outer equatorial radius
B_CUP = 17.6           # cup outer polar semi-axis (vertical)
A_BORE = 6.5           # cup bore equatorial radius
B_BORE = 11.9          # cup bore polar semi-axis
MOUTH_TILT = 43.5      # tilt of the cup mouth plane from horizontal (deg); plane passes through cup centre
# rows: (radius of cup centre from vase axis, height of cup centre)
ROWS = [
    (39.1, 67.75),
    (41.0, 46.55),
    (38.1, 25.4),
]
SEAM_ANGLE = 100.0     # where the revolve seam of the body is parked (cosmetic only)

# ---------------- body of revolution ----------------
# The neck is one concave arc (centre at height Z_NECK_MIN, radius Ra) touching the bulb ellipse at
# parameter th:  P(th) = (A cos th, Zc + B sin th), outward normal n(th) ~ (B cos th, A sin th),
# and  P + Ra * n_hat = (R_NECK_MIN + Ra, Z_NECK_MIN).
def _neck_arc(th):
    nx, nz = B_BULB * math.cos(th), A_BULB * math.sin(th)
    nl = math.hypot(nx, nz)
    nx, nz = nx / nl, nz / nl
    ra = (Z_NECK_MIN - Z_BULB - B_BULB * math.sin(th)) / nz
    f = A_BULB * math.cos(th) + ra * (nx - 1.0) - R_NECK_MIN
    return f, ra


lo, hi = 1e-3, math.pi / 2 - 1e-3
for _ in range(200):  # bisection for the tangency parameter
    mid = 0.5 * (lo + hi)
    if (_neck_arc(lo)[0] > 0) == (_neck_arc(mid)[0] > 0):
        lo = mid
    else:
        hi = mid
th1 = 0.5 * (lo + hi)
Ra = _neck_arc(th1)[1]
cx, cz = R_NECK_MIN + Ra, Z_NECK_MIN                             # neck arc centre
tx, tz = A_BULB * math.cos(th1), Z_BULB + B_BULB * math.sin(th1)  # bulb / neck tangent point

th0 = math.asin(-Z_BULB / B_BULB)                 # foot edge on the bulb ellipse
r_foot = A_BULB * math.cos(th0)
r_top = cx - math.sqrt(Ra ** 2 - (H_TOTAL - cz) ** 2)

b0 = math.atan2(tz - cz, tx - cx) % (2 * math.pi)
b1 = math.atan2(H_TOTAL - cz, r_top - cx) % (2 * math.pi)
bm = 0.5 * (b0 + b1)
m2 = (cx + Ra * math.cos(bm), cz + Ra * math.sin(bm))

profile = (
    cq.Workplane("XZ")
    .moveTo(0, 0)
    .lineTo(r_foot, 0)
    .ellipseArc(A_BULB, B_BULB, math.degrees(th0), math.degrees(th1), startAtCurrent=True)
    .threePointArc(m2, (r_top, H_TOTAL))
    .lineTo(0, H_TOTAL)
    .close()
)
body = profile.revolve(360.0, (0, 0, 0), (0, 1, 0)).rotate((0, 0, 0), (0, 0, 1), SEAM_ANGLE)


# ---------------- egg cups ----------------
def ellipsoid_solid(a, b, seam_angle):
    """Solid ellipsoid of revolution about Z, centred at the origin (revolved half ellipse)."""
    return (
        cq.Workplane("XZ")
        .moveTo(0, -b)
        .ellipseArc(a, b, -90, 90, startAtCurrent=True)
        .close()
        .revolve(360.0, (0, 0, 0), (0, 1, 0))
        .val()
        # park the revolve seam where it is out of sight (cosmetic only)
        .rotate(cq.Vector(0, 0, 0), cq.Vector(0, 0, 1), seam_angle)
    )


def make_cup(rc, zc):
    """Hollow egg cup: ellipsoid shell, top cut off by a plane through its centre tilted outward."""
    outer = ellipsoid_solid(A_CUP, B_CUP, 180.0)
    inner = ellipsoid_solid(A_BORE, B_BORE, 0.0)
    cup = outer.cut(inner)
    t = math.radians(MOUTH_TILT)
    n = cq.Vector(math.sin(t), 0, math.cos(t))
    pl = cq.Plane(origin=cq.Vector(0, 0, 0), xDir=cq.Vector(math.cos(t), 0, -math.sin(t)), normal=n)
    cutter = cq.Workplane(pl).rect(80, 80).extrude(40).val()
    cup = cup.cut(cutter)
    return cup.translate(cq.Vector(rc, 0, zc))


# 3 rows x N_CUPS egg cups, polar pattern about the vase axis, fused to the body in one boolean
cups = []
for rc, zc in ROWS:
    base = make_cup(rc, zc)
    for k in range(N_CUPS):
        cups.append(base.rotate(cq.Vector(0, 0, 0), cq.Vector(0, 0, 1), 360.0 / N_CUPS * k))
result = cq.Workplane("XY").add(body.val().fuse(*cups).clean())

# neck bore (flat bottomed)
result = result.cut(
    cq.Workplane("XY").workplane(offset=Z_HOLE_BOTTOM).circle(R_HOLE).extrude(H_TOTAL)
)

# small centre mark in the underside of the foot
result = result.cut(cq.Workplane("XY").circle(R_DIMPLE).extrude(D_DIMPLE))
